import math
import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- driving dimensions (mm) ----------------
T = 4.7                 # total plate thickness
N_LAYERS = 5            # laminated look: stack of sheets with rounded edges
LAYER_R = 0.35          # edge round of every sheet
LAYER_STEP = 0.3        # every lower sheet sticks out a little further

# half-outline (right side, +X), listed from top (+Y) to bottom (-Y)
HEAD_TOP_Y = 117.9
HEAD_TOP_HW = 62.9      # half width of the top edge
HEAD_MAX_Y = 80.1
HEAD_MAX_HW = 76.3      # widest point of the head
NOTCH1_Y = 64.3
NOTCH1_HW = 35.9
SHOULDER_Y = 39.8
SHOULDER_HW = 45.7
NECK_Y = 25.1
NECK_HW = 9.7
BODY_Y1 = -46.2
BODY_HW = 40.0
BODY_HW2 = 40.6      # body flares slightly toward its lower corner
BODY_Y2 = -60.1
WAIST_Y = -83.9
WAIST_HW = 9.4
TAIL_Y = -117.8
TAIL_HW = 34.6
HEAD_EXT = (N_LAYERS - 1) / 2.0 * LAYER_STEP  # head top: top sheet edge lands on HEAD_TOP_Y
# notch in the lower sheets at the middle of the head top edge
HN_X0, HN_X1 = -22.0, -3.0
HN_DEPTH = 5.0
HN_LAYERS = 3

HOLE_D = 4.0
HOLE1_Y = 107.7
HOLE2_Y = 32.0

# square window in the body
SQ_W = 26.0
SQ_H = 27.0
SQ_TOP_Y = -32.8
SQ_NOTCH_W = 12.0
SQ_NOTCH_D = 3.0

SQ_CB = 1.5            # bottom counterbore around the window (per side)
SQ_CB_DEPTH = 3 * T / N_LAYERS

# blind features on the underside
BOT_HOLES = [(-20.8, 61.5), (-4.6, 62.2)]
BOT_HOLE_D = 4.6
BOT_HOLE_DEPTH = 1.2
TAIL_RECESS = (0.0, -95.8)
TAIL_RECESS_D = 8.5
TAIL_RECESS_DEPTH = 1.0

# small flat patches on the grooved side walls
EDGE_PAD_L = 5.5
EDGE_PAD_H = 1.3
EDGE_PAD_W = 1.0
EDGE_PAD_OUT = -0.2                      # outer face, relative to the nominal outline
EDGE_PAD_Z = T - 1.6 * T / N_LAYERS      # around the second sheet from the top

# keyed slot in the head (aligned with the lower-right head edge)
SLOT_ANG = 20.5
SLOT_V = 68.4           # offset of slot axis from origin (perpendicular)
SLOT_U0 = 48.5          # start of wide part along slot axis
SLOT_U1 = 78.5          # wide -> narrow step
SLOT_U2 = 93.3          # end of narrow part
SLOT_WIDE = 24.0
SLOT_NARROW = 16.0
SLOT_NARROW_OFF = 0.7    # narrow part sits slightly toward the +v side
SLOT_R = 6.0            # round at the closed wide end
SLOT_R2 = 1.5           # corners of the narrow end
SLOT_R3 = 2.2           # corners of the wide/narrow step (-v side)
SLOT_R4 = 1.4           # corners of the wide/narrow step (+v side, smaller step)


def outline_pts(tail_ext=0.0, head_ext=0.0):
    # tail tips / head top corners pushed further out along their side edges
    # so that the two ends can be trimmed flat afterwards
    k = (TAIL_HW - WAIST_HW) / (WAIST_Y - TAIL_Y)
    kh = (HEAD_TOP_HW - HEAD_MAX_HW) / (HEAD_TOP_Y - HEAD_MAX_Y)
    right = [
        (HEAD_TOP_HW + kh * head_ext, HEAD_TOP_Y + head_ext),
        (HEAD_MAX_HW, HEAD_MAX_Y),
        (NOTCH1_HW, NOTCH1_Y),
        (SHOULDER_HW, SHOULDER_Y),
        (NECK_HW, NECK_Y),
        (BODY_HW, BODY_Y1),
        (BODY_HW2, BODY_Y2),
        (WAIST_HW, WAIST_Y),
        (TAIL_HW + k * tail_ext, TAIL_Y - tail_ext),
    ]
    left = [(-x, y) for (x, y) in reversed(right)]
    return right + left


# ---------------- laminated plate ----------------
t_layer = T / N_LAYERS
base_wire = cq.Wire.makePolygon(
    [cq.Vector(x, y, 0) for (x, y) in outline_pts(tail_ext=LAYER_R + 2.0, head_ext=HEAD_EXT)],
    close=True,
)
plate = None
for i in range(N_LAYERS):
    off = ((N_LAYERS - 1) / 2.0 - i) * LAYER_STEP   # bottom sheet is the largest
    w = base_wire.offset2D(off, kind="intersection")[0] if off != 0 else base_wire
    layer = (
        cq.Workplane("XY")
        .add(cq.Face.makeFromWires(w))
        .wires().toPending()
        .extrude(t_layer)
        .translate((0, 0, i * t_layer))
    )
    layer = layer.edges("not |Z").fillet(LAYER_R)
    plate = layer if plate is None else plate.union(layer)

# trim the tail end flat
trim = (
    cq.Workplane("XY")
    .center(0, TAIL_Y - 10)
    .rect(200, 20)
    .extrude(T + 2)
    .translate((0, 0, -1))
)
plate = plate.cut(trim)
# trim the head top edge flat (the rounded top sheet just touches the plane)
trim_h = (
    cq.Workplane("XY")
    .center(0, HEAD_TOP_Y + 10)
    .rect(200, 20)
    .extrude(T + 2)
    .translate((0, 0, -1))
)
plate = plate.cut(trim_h)
# notch in the lower sheets of the head top edge
head_notch = (
    cq.Workplane("XY")
    .center((HN_X0 + HN_X1) / 2, HEAD_TOP_Y - HN_DEPTH / 2 + 1)
    .rect(HN_X1 - HN_X0, HN_DEPTH + 2)
    .extrude(HN_LAYERS * T / N_LAYERS + 1)
    .translate((0, 0, -1))
)
plate = plate.cut(head_notch)

# ---------------- through holes ----------------
holes = (
    cq.Workplane("XY")
    .pushPoints([(0, HOLE1_Y), (0, HOLE2_Y)])
    .circle(HOLE_D / 2)
    .extrude(T + 2)
    .translate((0, 0, -1))
)
plate = plate.cut(holes)

# ---------------- square window with small notch ----------------
sq = (
    cq.Workplane("XY")
    .center(0, SQ_TOP_Y - SQ_H / 2)
    .rect(SQ_W, SQ_H)
    .extrude(T + 2)
    .translate((0, 0, -1))
)
sqn = (
    cq.Workplane("XY")
    .center(0, SQ_TOP_Y - SQ_H)
    .rect(SQ_NOTCH_W, 2 * SQ_NOTCH_D)
    .extrude(T + 2)
    .translate((0, 0, -1))
)
cb = (
    cq.Workplane("XY")
    .center(0, SQ_TOP_Y - SQ_H / 2)
    .rect(SQ_W + 2 * SQ_CB, SQ_H + 2 * SQ_CB)
    .extrude(SQ_CB_DEPTH + 1)
    .translate((0, 0, -1))
)
plate = plate.cut(sq.union(sqn).union(cb))

# ---------------- blind features on the underside ----------------
bh = (
    cq.Workplane("XY")
    .pushPoints(BOT_HOLES)
    .circle(BOT_HOLE_D / 2)
    .extrude(BOT_HOLE_DEPTH + 1)
    .translate((0, 0, -1))
)
tr = (
    cq.Workplane("XY")
    .center(*TAIL_RECESS)
    .circle(TAIL_RECESS_D / 2)
    .extrude(TAIL_RECESS_DEPTH + 1)
    .translate((0, 0, -1))
)
plate = plate.cut(bh).cut(tr)

# ---------------- small flat patches on the grooved side walls ----------------
P = outline_pts()


def edge_pad(ia, ib, x_at):
    """small flat patch bridging the sheet grooves on a side wall"""
    (xa, ya), (xb, yb) = P[ia], P[ib]
    s_ = (x_at - xa) / (xb - xa)
    px, py = xa + s_ * (xb - xa), ya + s_ * (yb - ya)
    L = math.hypot(xb - xa, yb - ya)
    nx, ny = -(yb - ya) / L, (xb - xa) / L          # outward normal (CW outline)
    ang = math.degrees(math.atan2(yb - ya, xb - xa))
    c = EDGE_PAD_OUT - EDGE_PAD_W / 2
    return (
        cq.Workplane("XY")
        .box(EDGE_PAD_L, EDGE_PAD_W, EDGE_PAD_H)
        .rotate((0, 0, 0), (0, 0, 1), ang)
        .translate((px + nx * c, py + ny * c, EDGE_PAD_Z))
    )


# indices: 0 head top R, 1 head max R, 2 notch R, 3 shoulder R, 4 neck R,
# 5 body R, 6 body R low, 7 waist R, 8 tail R, then mirrored (9..17)
PAD_HEAD_X = 53.0
PAD_SHOULDER_X = 26.9
PAD_BODY_X = 25.0
pads = [
    edge_pad(1, 2, PAD_HEAD_X),          # lower right head edge
    edge_pad(3, 4, PAD_SHOULDER_X),      # right shoulder -> neck
    edge_pad(6, 7, PAD_BODY_X),          # right lower body
    edge_pad(15, 16, -PAD_HEAD_X),       # lower left head edge
    edge_pad(13, 14, -PAD_SHOULDER_X),   # neck -> left shoulder
    edge_pad(10, 11, -PAD_BODY_X),       # left lower body
]
for pd in pads:
    plate = plate.union(pd)

# ---------------- keyed slot ----------------
a = math.radians(SLOT_ANG)
ux, uy = math.cos(a), math.sin(a)
vx, vy = -math.sin(a), math.cos(a)


def uv(u, v):
    return (u * ux + v * vx, u * uy + v * vy)


def fillet_near(wp, pts, r, tol=0.5):
    """fillet the vertical edges of wp located at the given XY points"""
    sel = []
    for e in wp.edges("|Z").vals():
        c = e.Center()
        if any(abs(c.x - px) < tol and abs(c.y - py) < tol for (px, py) in pts):
            sel.append(e)
    return wp.newObject(sel).fillet(r)


hw, hn = SLOT_WIDE / 2, SLOT_NARROW / 2
vn = SLOT_V + SLOT_NARROW_OFF
slot_uv = [
    (SLOT_U0, SLOT_V - hw), (SLOT_U1, SLOT_V - hw),
    (SLOT_U1, vn - hn), (SLOT_U2, vn - hn),
    (SLOT_U2, vn + hn), (SLOT_U1, vn + hn),
    (SLOT_U1, SLOT_V + hw), (SLOT_U0, SLOT_V + hw),
]
slot = (
    cq.Workplane("XY")
    .polyline([uv(u, v) for (u, v) in slot_uv]).close()
    .extrude(T + 2)
    .translate((0, 0, -1))
)
slot = fillet_near(slot, [uv(SLOT_U0, SLOT_V - hw), uv(SLOT_U0, SLOT_V + hw)], SLOT_R)
slot = fillet_near(slot, [uv(SLOT_U1, SLOT_V - hw), uv(SLOT_U1, vn - hn)], SLOT_R3)
slot = fillet_near(slot, [uv(SLOT_U1, SLOT_V + hw), uv(SLOT_U1, vn + hn)], SLOT_R4)
slot = fillet_near(slot, [uv(SLOT_U2, vn - hn), uv(SLOT_U2, vn + hn)], SLOT_R2)
plate = plate.cut(slot)

# ---------------- seam lines of the laminate (very fine grooves) ----------------
SEAM_W = 0.3
SEAM_D = 0.25
A_, B_ = BOT_HOLES
top_seams = [
    ((SQ_W / 2, SQ_TOP_Y), (BODY_HW + 3.0, SQ_TOP_Y)),          # window -> right edge
    (uv(SLOT_U2, vn), uv(SLOT_U2 + 12.0, vn)),                 # slot end -> head edge
]
bot_seams = [
    ((SQ_W / 2 + SQ_CB, -60.0), (BODY_HW2 + 3.0, -60.0)),      # window -> body corner
    ((0.0, -99.7), (25.0, -99.7)),                             # tail recess -> tail edge
    (A_, B_),
    (A_, (SHOULDER_HW, SHOULDER_Y)),
    (B_, (NOTCH1_HW, NOTCH1_Y)),
    ((-25.0, 76.5), (0.0, 76.5)),                              # pad outline
    ((0.0, 76.5), (0.0, 100.5)),
    ((0.0, 100.5), (-25.0, 100.5)),
    ((-25.0, 100.5), (-25.0, 76.5)),
    ((-25.0, 100.5), (HN_X0, HEAD_TOP_Y - HN_DEPTH)),          # pad -> head notch
    ((0.0, 100.5), (0.0, HOLE1_Y)),
    ((0.0, HOLE1_Y), (HN_X1, HEAD_TOP_Y - HN_DEPTH)),
    ((0.0, 76.5), (23.5, 76.5)),                               # pad -> slot
]


def seam(p0, p1, on_top):
    (x0, y0), (x1, y1) = p0, p1
    L = math.hypot(x1 - x0, y1 - y0)
    ang = math.degrees(math.atan2(y1 - y0, x1 - x0))
    zc = T - SEAM_D / 2 + 0.5 if on_top else SEAM_D / 2 - 0.5
    return (
        cq.Workplane("XY")
        .box(L, SEAM_W, SEAM_D + 1.0)
        .rotate((0, 0, 0), (0, 0, 1), ang)
        .translate(((x0 + x1) / 2, (y0 + y1) / 2, zc))
    )


seams = None
for (p0, p1) in top_seams:
    g = seam(p0, p1, True)
    seams = g if seams is None else seams.union(g)
for (p0, p1) in bot_seams:
    seams = seams.union(seam(p0, p1, False))
plate = plate.cut(seams)

result = plate
